import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_PLATES = 5          # number of separate plates
PITCH = 61.25         # centre-to-centre spacing along X
W = 54.0              # plate width  (X)
H = 90.0              # plate height (Z)
T_BASE = 1.95         # base plate thickness (Y)
RIM_W = 2.0           # raised border width
RIM_H = 1.75          # raised border height above base face

# logo (raised square pad with 2x2 letter pockets, top right)
LOGO_CX = 14.6        # logo centre, relative to plate centre
LOGO_CZ = 32.0
LOGO_ANG = 20.0       # CCW rotation seen from the front
LOGO_S = 20.0         # pad size
LOGO_FW = 1.3         # pad border left of / above the pockets
CELL_GAP = 1.0        # web between neighbouring pockets
CELL_W = 7.9          # letter pocket width
CELL_HT = 8.2         # letter pocket height
LOGO_H = 0.8          # pad height above the plate face
POCKET_D = 0.5        # letter pocket depth (letters rise back to the pad top)
LET_H = 7.0           # letter height
LET_SW = 1.0          # letter stroke width

# oval emblem (bottom centre)
OV_CX = 0.3           # emblem centre, relative to plate centre
OV_CZ = -28.2
OV_A = 5.8            # outer semi-axis X
OV_B = 8.3            # outer semi-axis Z
OV_RING = 2.0         # ring width
OV_BAR_W = 1.9        # bar width
OV_BAR_ANG = 37.0     # bar angle from X
OV_H = 1.5            # emblem relief height

VIEW = {"azimuth": 45, "elevation": 26}


def front_plane(x, z, ang=0.0):
    """Workplane on the plate front face (normal -Y), rotated ang deg CCW."""
    a = math.radians(ang)
    return cq.Workplane(cq.Plane(origin=(x, -T_BASE, z),
                                 xDir=(math.cos(a), 0, math.sin(a)),
                                 normal=(0, -1, 0)))


def ell_band(wp, cx, cy, a, b, sw, a1, a2, h):
    """Stroke of width sw along the ellipse (semi-axes a, b) from a1 to a2 deg (CCW)."""
    ring = (wp.center(cx, cy).ellipse(a + sw / 2, b + sw / 2).extrude(h)
            .cut(wp.center(cx, cy).ellipse(a - sw / 2, b - sw / 2).extrude(h)))
    # wedge selecting the angular range
    r = 3 * (max(a, b) + sw)
    n = max(2, int(math.ceil((a2 - a1) / 60.0)))
    pts = [(cx, cy)] + [(cx + r * math.cos(math.radians(a1 + (a2 - a1) * i / n)),
                         cy + r * math.sin(math.radians(a1 + (a2 - a1) * i / n)))
                        for i in range(n + 1)]
    wedge = wp.polyline(pts).close().extrude(h)
    return ring.intersect(wedge)


def box2d(wp, cx, cy, w, h2, h):
    return wp.center(cx, cy).rect(w, h2).extrude(h)


def letter_S(wp, h):
    sw = LET_SW
    b = (LET_H - sw) / 4.0
    a = (LET_H * 0.64 - sw) / 2.0
    top = ell_band(wp, 0, b, a, b, sw, 25, 270, h)
    bot = ell_band(wp, 0, -b, a, b, sw, 205, 450, h)
    return top.union(bot)


def letter_I(wp, h):
    sw = LET_SW
    wi = LET_H * 0.52
    s = box2d(wp, 0, 0, sw, LET_H, h)
    s = s.union(box2d(wp, 0, LET_H / 2 - sw / 2, wi, sw, h))
    s = s.union(box2d(wp, 0, -LET_H / 2 + sw / 2, wi, sw, h))
    return s


def letter_J(wp, h):
    sw = LET_SW
    wj = LET_H * 0.565
    xr = wj / 2                      # right edge of the stem
    xs = xr - sw / 2                 # stem centre line
    a = (wj - sw) / 2                # hook radii (centre line)
    b = LET_H * 0.21
    xc = xs - a
    yc = -LET_H / 2 + sw / 2 + b
    s = box2d(wp, xs, (LET_H / 2 + yc) / 2, sw, LET_H / 2 - yc, h)
    tb = LET_H * 0.39
    s = s.union(box2d(wp, xr - tb / 2, LET_H / 2 - sw / 2, tb, sw, h))
    s = s.union(ell_band(wp, xc, yc, a, b, sw, 180, 360, h))
    return s


def letter_P(wp, h):
    sw = LET_SW
    wp_ = LET_H * 0.63
    xl = -wp_ / 2 + sw / 2           # stem centre line
    bb = (LET_H * 0.56 - sw) / 2     # bowl half height (centre line)
    ab = bb * 0.95
    xc = wp_ / 2 - sw / 2 - ab
    yc = LET_H / 2 - sw / 2 - bb
    s = box2d(wp, xl, 0, sw, LET_H, h)
    s = s.union(box2d(wp, (xl + xc) / 2, yc + bb, xc - xl, sw, h))
    s = s.union(box2d(wp, (xl + xc) / 2, yc - bb, xc - xl, sw, h))
    s = s.union(ell_band(wp, xc, yc, ab, bb, sw, -90, 90, h))
    return s


def make_logo():
    wp = front_plane(LOGO_CX, LOGO_CZ, LOGO_ANG)
    logo = wp.rect(LOGO_S, LOGO_S).extrude(LOGO_H)
    x0 = -LOGO_S / 2 + LOGO_FW + CELL_W / 2          # left pocket column centre
    y0 = LOGO_S / 2 - LOGO_FW - CELL_HT / 2          # top pocket row centre
    dx, dy = CELL_W + CELL_GAP, CELL_HT + CELL_GAP
    # (column, row): (letter builder, horizontal glyph offset as fraction of LET_H)
    letters = {(0, 0): (letter_S, 0.0), (1, 0): (letter_I, 0.0),
               (0, 1): (letter_J, -0.056), (1, 1): (letter_P, 0.034)}
    for (ix, iy), (fn, gx) in letters.items():
        cx, cy = x0 + ix * dx, y0 - iy * dy
        cell_wp = cq.Workplane(cq.Plane(origin=wp.plane.toWorldCoords((cx, cy)),
                                        xDir=wp.plane.xDir, normal=wp.plane.zDir))
        let_wp = cq.Workplane(cq.Plane(origin=wp.plane.toWorldCoords((cx + gx * LET_H, cy)),
                                       xDir=wp.plane.xDir, normal=wp.plane.zDir))
        pocket = (cell_wp.workplane(offset=LOGO_H - POCKET_D)
                  .rect(CELL_W, CELL_HT).extrude(POCKET_D))
        letter = fn(let_wp.workplane(offset=LOGO_H - POCKET_D), POCKET_D)
        logo = logo.cut(pocket).union(letter)
    # keep the relief inside the plate outline
    clip = front_plane(0, 0).rect(W, H).extrude(LOGO_H)
    return logo.intersect(clip)


def make_oval():
    wp = front_plane(OV_CX, OV_CZ)
    ring = (wp.ellipse(OV_A, OV_B).ellipse(OV_A - OV_RING, OV_B - OV_RING).extrude(OV_H))
    disk = wp.ellipse(OV_A - OV_RING / 2, OV_B - OV_RING / 2).extrude(OV_H)
    bar = (front_plane(OV_CX, OV_CZ, OV_BAR_ANG).rect(3 * OV_B, OV_BAR_W).extrude(OV_H)).intersect(disk)
    return ring.union(bar)


def make_plate():
    base = cq.Workplane("XZ").rect(W, H).extrude(T_BASE)
    rim = front_plane(0, 0).rect(W, H).rect(W - 2 * RIM_W, H - 2 * RIM_W).extrude(RIM_H)
    plate = base.union(rim).union(make_logo()).union(make_oval())
    return plate


plate = make_plate().val()
solids = []
for i in range(N_PLATES):
    x = (i - (N_PLATES - 1) / 2.0) * PITCH
    solids.append(plate.translate(cq.Vector(x, 0, 0)))
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])
